import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 110.0      # X
PLATE_W = 80.0       # Y
PLATE_T = 2.8        # plate thickness
EDGE_R = 0.4         # top outer edge round
CORNER_R = 1.0       # vertical corner round

# raised embossed rims around the slots
BOSS_H = 0.9        # height above plate top
BOSS_MARGIN = 2.4    # rim width around the slot (footprint)
BOSS_TAPER = 62.0    # draft of the rim flanks (deg from vertical)
BOSS_TOP_R = 0.3     # round on the rim crest
BOSS_BASE_R = 0.5    # concave round at the rim foot

SLOT_W = 4.8
SLOT_R = 0.35
# (cx, cy, length, along_x)
SLOTS = [
    (-7.65, 31.2, 77.1, True),
    (-7.65, 5.2, 77.1, True),
    (42.5, 6.5, 34.1, False),
]

# plain rectangular window
WIN_CX, WIN_CY, WIN_L, WIN_W = -18.7, -12.5, 57.0, 10.1
WIN_EDGE_R = 0.5
WIN_R = 0.5          # window corner radius

# round hole
HOLE_X, HOLE_Y, HOLE_D = 26.2, -27.7, 8.5
HOLE_EDGE_R = 0.2

# feet
FOOT_S = 7.3
FOOT_INSET = 3.3
FOOT_H = 7.7
FOOT_R = 0.8         # outer vertical corner rounds
FOOT_INNER_R = 4.0   # big round on the corner facing the plate centre
FOOT_BOT_R = 0.5
PIN_D = 3.1
PIN_H = 0.4

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(PLATE_L, PLATE_W)
    .extrude(PLATE_T)
    .edges("|Z").fillet(CORNER_R)
    .faces(">Z").edges().fillet(EDGE_R)
)

# ---------------- embossed rims ----------------
for cx, cy, ln, along_x in SLOTS:
    bl = ln + 2 * BOSS_MARGIN
    bw = SLOT_W + 2 * BOSS_MARGIN
    sx, sy = (bl, bw) if along_x else (bw, bl)
    sk = cq.Sketch().rect(sx, sy).vertices().fillet(BOSS_MARGIN + SLOT_R)
    boss = (
        cq.Workplane("XY")
        .workplane(offset=PLATE_T - 0.02)
        .center(cx, cy)
        .placeSketch(sk)
        .extrude(BOSS_H + 0.02, taper=BOSS_TAPER)
        .faces(">Z").edges().fillet(BOSS_TOP_R)
    )
    plate = plate.union(boss)
    # concave round where the rim meets the plate
    plate = plate.edges(
        cq.selectors.BoxSelector(
            (cx - sx / 2 - 0.5, cy - sy / 2 - 0.5, PLATE_T - 0.05),
            (cx + sx / 2 + 0.5, cy + sy / 2 + 0.5, PLATE_T + 0.05),
        )
    ).fillet(BOSS_BASE_R)

# ---------------- feet ----------------
def foot_solid(px, py, sx, sy):
    """Square foot whose corner facing the plate centre carries a big round."""
    a = FOOT_S / 2
    R, r = FOOT_INNER_R, FOOT_R
    k = 1 - 1 / math.sqrt(2)

    def p(x, y):
        return (px + sx * x, py + sy * y)

    wp = (
        cq.Workplane("XY")
        .workplane(offset=0.01)
        .moveTo(*p(-a + R, -a))
        .lineTo(*p(a - r, -a))
        .threePointArc(p(a - r * k, -a + r * k), p(a, -a + r))
        .lineTo(*p(a, a - r))
        .threePointArc(p(a - r * k, a - r * k), p(a - r, a))
        .lineTo(*p(-a + r, a))
        .threePointArc(p(-a + r * k, a - r * k), p(-a, a - r))
        .lineTo(*p(-a, -a + R))
        .threePointArc(p(-a + R * k, -a + R * k), p(-a + R, -a))
        .close()
    )
    foot = wp.extrude(-FOOT_H - 0.01).faces("<Z").edges().fillet(FOOT_BOT_R)
    pin = (
        cq.Workplane("XY")
        .workplane(offset=-FOOT_H + 0.01)
        .center(px, py)
        .circle(PIN_D / 2)
        .extrude(-PIN_H - 0.01)
    )
    return foot.union(pin)


fx = PLATE_L / 2 - FOOT_INSET - FOOT_S / 2
fy = PLATE_W / 2 - FOOT_INSET - FOOT_S / 2
for sx in (-1, 1):
    for sy in (-1, 1):
        plate = plate.union(foot_solid(sx * fx, sy * fy, sx, sy))

# ---------------- through cuts ----------------
cut_h = 20.0
for cx, cy, ln, along_x in SLOTS:
    sx, sy = (ln, SLOT_W) if along_x else (SLOT_W, ln)
    slot = (
        cq.Workplane("XY")
        .workplane(offset=-5)
        .center(cx, cy)
        .rect(sx, sy)
        .extrude(cut_h)
        .edges("|Z").fillet(SLOT_R)
    )
    plate = plate.cut(slot)

win = (
    cq.Workplane("XY")
    .workplane(offset=-5)
    .center(WIN_CX, WIN_CY)
    .rect(WIN_L, WIN_W)
    .extrude(cut_h)
    .edges("|Z").fillet(WIN_R)
)
plate = plate.cut(win)

# round the top edge of the window
plate = plate.edges(
    cq.selectors.BoxSelector(
        (WIN_CX - WIN_L / 2 - 1, WIN_CY - WIN_W / 2 - 1, PLATE_T - 0.1),
        (WIN_CX + WIN_L / 2 + 1, WIN_CY + WIN_W / 2 + 1, PLATE_T + 0.1),
    )
).fillet(WIN_EDGE_R)

hole = (
    cq.Workplane("XY")
    .workplane(offset=-5)
    .center(HOLE_X, HOLE_Y)
    .circle(HOLE_D / 2)
    .extrude(cut_h)
)
plate = plate.cut(hole)
plate = plate.edges(
    cq.selectors.BoxSelector(
        (HOLE_X - HOLE_D, HOLE_Y - HOLE_D, PLATE_T - 0.1),
        (HOLE_X + HOLE_D, HOLE_Y + HOLE_D, PLATE_T + 0.1),
    )
).fillet(HOLE_EDGE_R)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
